import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 175.0        # outer width  (X)
D = 153.0        # outer depth  (Y)
H = 236.5        # outer height (Z)
R_OUT = 7.0      # fillet on the outer edges running along X
T_SIDE = 6.0     # side wall thickness
T_TB = 10.4      # top / bottom wall thickness
R_IN = 3.5       # inner floor-to-wall fillet (edges along Y, middle section)
R_IN_TOP = 6.0   # inner ceiling-to-wall fillet (edges along Y, middle section)
Z_F = 6.2        # depth of the sharp-cornered front / back mouth zones

# mouth groove profile (also the side-wall notch in front of each seal ear)
N_Z0 = T_TB      # mouth floor height at the mouth face
N_Z1 = 6.6       # mouth floor height at the step (sloped floor/ceiling)

# recessed front panel
P_SET = 27.8     # set-back of the panel front face from the front face
T_P = 11.0       # panel thickness
SLOT_H = 9.6     # height of the through slot above the panel
PB_Z = 79.4      # height of the panel's lower edge (top of lower opening)
PB_R = 3.0       # rounding of the lower opening's upper corners
WIN_X = 74.3     # half width of the window recess
WIN_Z0 = 98.7    # window recess bottom
WIN_Z1 = 197.9   # window recess top
WIN_D = 4.0      # window recess depth

# floor recess in the lower compartment (back / right part)
FR_X0 = -62.9    # left boundary of the floor recess
FR_Y0 = -5.6     # front boundary of the floor recess
FR_D = 4.9       # recess depth

# thin vertical pins at the back of the lower compartment
PIN_XR = 77.0    # x of the right pin axis
PIN_YR = 67.0    # y of the right pin axis
PIN_XL = -76.8   # x of the left pin axis
PIN_YL = 60.0    # y of the left pin axis
PIN_D = 1.5      # pin diameter
PIN_Z = 49.0     # pin top height

# seal ears
EAR_Z = H / 2.0
EAR_OUT = 11.3   # protrusion from side wall
EAR_HH = 7.8     # half height of ear
EAR_T = 5.8      # ear thickness (Y)
HOLE_HH = 3.9    # half height of seal hole
HOLE_L = 7.8     # hole length from wall
EAR_RF = 0.8     # blend radius where the ear meets the wall

IW = W - 2 * T_SIDE
IH = H - 2 * T_TB

# ---------------- outer sleeve ----------------
outer = (
    cq.Workplane("XY")
    .box(W, D, H, centered=(True, True, False))
    .edges("|X")
    .fillet(R_OUT)
)

# middle cavity with rounded inner corners
mid = (
    cq.Workplane("XY")
    .box(IW, D - 2 * Z_F, IH, centered=(True, True, False))
    .translate((0, 0, T_TB))
    .edges("|Y and >Z")
    .fillet(R_IN_TOP)
    .edges("|Y and <Z")
    .fillet(R_IN)
)
# mouth zones at front and back: sharp-cornered openings whose floor and ceiling
# slope outward (a wedge groove for the cover lip).  On the ear side the mouth
# also runs straight through the side wall (notch in front of the seal ear).
def mouth(side):
    """side=+1: front mouth with right-hand notch; side=-1: back mouth with left notch."""
    y_face = -D / 2 if side > 0 else D / 2       # mouth face
    y_in = y_face + side * Z_F                   # step back to the middle cavity
    y_out = y_face - side * 2.0                  # beyond the mouth
    pts = [
        (y_out, N_Z0),
        (y_face, N_Z0),
        (y_in, N_Z1),
        (y_in, H - N_Z1),
        (y_face, H - N_Z0),
        (y_out, H - N_Z0),
    ]
    if side > 0:
        x0, x1 = -IW / 2.0, W / 2.0 + 1.0
    else:
        x0, x1 = -W / 2.0 - 1.0, IW / 2.0
    return (
        cq.Workplane("YZ", origin=(x0, 0, 0))
        .polyline(pts)
        .close()
        .extrude(x1 - x0)
    )


# floor recess (lower level in the back/right part of the floor)
fr_w = (IW / 2.0 - R_IN) - FR_X0
fr_len = (D / 2 - Z_F) - FR_Y0
frec = (
    cq.Workplane("XY")
    .box(fr_w, fr_len, FR_D + 0.5, centered=False)
    .translate((FR_X0, FR_Y0, T_TB - FR_D))
)
body = (
    outer.cut(mid)
    .cut(mouth(+1))
    .cut(mouth(-1))
    .cut(frec)
)

# thin vertical pins at the back of the lower compartment
for px, py in ((PIN_XR, PIN_YR), (PIN_XL, PIN_YL)):
    pin = (
        cq.Workplane("XY", origin=(px, py, T_TB - FR_D - 1.0))
        .circle(PIN_D / 2.0)
        .extrude(PIN_Z - (T_TB - FR_D - 1.0))
    )
    body = body.union(pin)

# ---------------- recessed front panel ----------------
py0 = -D / 2 + P_SET
panel = (
    cq.Workplane("XY")
    .box(IW + 1.0, T_P, IH + 1.0, centered=(True, False, False))
    .translate((0, py0, T_TB - 0.5))
)
# top slot (stadium through the panel)
slot_cz = H - T_TB - SLOT_H / 2.0
slot = (
    cq.Workplane("XZ", origin=(0, py0 - 1, 0))
    .center(0, slot_cz)
    .slot2D(IW, SLOT_H)
    .extrude(-(T_P + 2))
)
# lower opening (through the panel only)
low_h = PB_Z - T_TB + 5
low = (
    cq.Workplane("XZ", origin=(0, py0 - 1, 0))
    .center(0, T_TB - 5 + low_h / 2.0)
    .rect(IW, low_h)
    .extrude(-(T_P + 2))
    .edges("|Y and >Z")
    .fillet(PB_R)
)
# window recess on the panel front
win = (
    cq.Workplane("XZ", origin=(0, py0 - 1, 0))
    .center(0, (WIN_Z0 + WIN_Z1) / 2.0)
    .rect(2 * WIN_X, WIN_Z1 - WIN_Z0)
    .extrude(-(WIN_D + 1))
)
panel = panel.cut(slot).cut(low).cut(win)
body = body.union(panel)


# ---------------- seal ears ----------------
def ear(side, y0):
    """U-shaped seal loop on a side wall.

    side = +1 (right wall) or -1 (left wall); y0 = ear start in Y (low side).
    The profile is drawn in the XZ plane: u = distance out of the wall, v = z - EAR_Z.
    """
    straight = EAR_OUT - EAR_HH          # straight part before the round end
    rf = EAR_RF                          # concave blend into the wall
    c45 = 1.0 - 0.70710678
    hh = EAR_HH

    def P(u, v):
        return (side * (W / 2.0 + u), EAR_Z + v)

    wp = cq.Workplane("XZ", origin=(0, y0, 0))
    outline = (
        wp.moveTo(*P(-1.0, hh + rf))
        .lineTo(*P(0.0, hh + rf))
        .threePointArc(P(rf * c45, hh + rf * c45), P(rf, hh))
        .lineTo(*P(straight, hh))
        .threePointArc(P(straight + hh, 0.0), P(straight, -hh))
        .lineTo(*P(rf, -hh))
        .threePointArc(P(rf * c45, -hh - rf * c45), P(0.0, -hh - rf))
        .lineTo(*P(-1.0, -hh - rf))
        .close()
        .extrude(-EAR_T)
    )
    hs = HOLE_L - HOLE_HH
    hole = (
        cq.Workplane("XZ", origin=(0, y0 - 1.0, 0))
        .moveTo(*P(-0.01, HOLE_HH))
        .lineTo(*P(hs, HOLE_HH))
        .threePointArc(P(hs + HOLE_HH, 0.0), P(hs, -HOLE_HH))
        .lineTo(*P(-0.01, -HOLE_HH))
        .close()
        .extrude(-(EAR_T + 2.0))
    )
    return outline.cut(hole)


ear_r = ear(+1, -D / 2 + Z_F)
ear_l = ear(-1, D / 2 - Z_F - EAR_T)
body = body.union(ear_r).union(ear_l)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
